import cadquery as cq

VIEW = {"azimuth": 45, "elevation": 26}

# =====================================================================
#  ESP8266 dev-board (NodeMCU style): PCB with 2 x 15 pin headers on top,
#  ESP-12 module, USB, buttons and SMD parts on the underside.
#  Board top face is z = 0, +Y points towards the USB end.
# =====================================================================

# ---------------- PCB ----------------
BOARD_W = 25.7          # X
BOARD_L = 48.4          # Y
BOARD_T = 1.6
CORNER_R = 2.5
HOLE_D = 3.3
HOLE_INSET_X = 2.5
HOLE_INSET_Y = 2.54

# ---------------- headers ----------------
PITCH = 2.54
N_PINS = 15
PIN_Y_OFFSET = 0.15    # header rows sit slightly towards the USB end
ROW_X_LEFT = -11.3
ROW_X_RIGHT = 10.98

HDR_H = 2.4             # plastic body height above board
HDR_GAP = 0.0           # gap between neighbouring plastic blocks
HDR_FILLET = 0.25
HDR_GROOVE_W = 1.9      # stand-off groove under every block (runs along Y)
HDR_GROOVE_D = 0.37

PIN_W = 0.64
PIN_TOP = 8.8           # tip height above board top
PIN_TAIL = 1.1          # length below board bottom
PIN_CH = 0.13           # tip chamfer

# ---------------- ESP-12 module ----------------
MOD_X0, MOD_X1 = -7.95, 8.65
MOD_L = 24.0
MOD_T = 1.3
SHIELD_X0, SHIELD_X1 = -5.78, 6.32
SHIELD_Y0, SHIELD_Y1 = -16.3, -1.1
SHIELD_T = 2.5
CAST_PITCH = 2.0        # castellated half-hole pads

# ---------------- micro USB ----------------
USB_CX = 0.6
USB_W = 7.8
USB_L = 5.0
USB_H = 2.35
USB_BEVEL = 0.6
USB_MOUTH_D = 4.0
USB_OVERHANG = 0.4

# tactile switches (reset / flash)
BUTTONS = ((-6.25, 21.5), (6.9, 21.5))
BTN_W = 2.8
BTN_L = 3.8
BTN_H = 1.1
BTN_ACT_D = 1.6
BTN_ACT_H = 0.9

ZB = -BOARD_T           # board bottom face


def box(cx, cy, z0, sx, sy, sz):
    """Box centred on (cx, cy) in plan, spanning z0 .. z0+sz (sz<0 hangs below)."""
    return cq.Workplane("XY").box(sx, sy, abs(sz)).translate((cx, cy, z0 + sz / 2.0))


def union_all(items, clean=True):
    out = None
    for it in items:
        out = it if out is None else out.union(it, clean=clean)
    return out


# =====================================================================
# PCB
# =====================================================================
hx = BOARD_W / 2 - HOLE_INSET_X
hy = BOARD_L / 2 - HOLE_INSET_Y
plate = (
    cq.Workplane("XY")
    .workplane(offset=ZB)
    .rect(BOARD_W, BOARD_L)
    .extrude(BOARD_T)
    .edges("|Z")
    .fillet(CORNER_R)
)
# the end strip between the two antenna-end holes is a separate face region
strip = box(0, (-BOARD_L / 2 - hy) / 2, ZB, 2 * hx, BOARD_L / 2 - hy, BOARD_T)
plate = plate.cut(strip).union(plate.intersect(strip), clean=False)
holes = (
    cq.Workplane("XY")
    .workplane(offset=ZB - 1)
    .pushPoints([(sx * hx, sy * hy) for sx in (-1, 1) for sy in (-1, 1)])
    .circle(HOLE_D / 2)
    .extrude(BOARD_T + 2)
)
board = plate.cut(holes, clean=False)

# =====================================================================
# Pin headers (plastic blocks + square pins)
# =====================================================================
pin_ys = [(i - (N_PINS - 1) / 2.0) * PITCH + PIN_Y_OFFSET for i in range(N_PINS)]

block = (
    cq.Workplane("XY")
    .box(PITCH, PITCH - HDR_GAP, HDR_H, centered=(True, True, False))
    .edges("|Z")
    .fillet(HDR_FILLET)
    .cut(cq.Workplane("XY").box(HDR_GROOVE_W, PITCH + 1, HDR_GROOVE_D, centered=(True, True, False)))
)

pin_len = PIN_TOP + BOARD_T + PIN_TAIL
pin = (
    cq.Workplane("XY")
    .box(PIN_W, PIN_W, pin_len, centered=(True, True, False))
    .faces(">Z or <Z").edges()
    .chamfer(PIN_CH)
    .translate((0, 0, ZB - PIN_TAIL))
)
unit = block.union(pin)

# blocks butt against each other; keep their individual faces (no face merging)
headers = union_all([unit.translate((x, y, 0)) for x in (ROW_X_LEFT, ROW_X_RIGHT) for y in pin_ys], clean=False)

# =====================================================================
# ESP-12 module on the underside
# =====================================================================
mod_y0 = -BOARD_L / 2 + 0.1
mod_cx = (MOD_X0 + MOD_X1) / 2
module = box(mod_cx, mod_y0 + MOD_L / 2, ZB, MOD_X1 - MOD_X0, MOD_L, -MOD_T)
shield = box((SHIELD_X0 + SHIELD_X1) / 2, (SHIELD_Y0 + SHIELD_Y1) / 2, ZB - MOD_T,
             SHIELD_X1 - SHIELD_X0, SHIELD_Y1 - SHIELD_Y0, -SHIELD_T)
module = module.union(shield)

# printed meander antenna on the exposed end of the module
ANT_N = 9
ANT_X0 = -2.2
ANT_PITCH = 0.7
ANT_Y0, ANT_Y1 = -23.4, -19.8
ANT_W = 0.25
ANT_T = 0.05
zt = ZB - MOD_T
ant = []
for i in range(ANT_N):
    ax = ANT_X0 + i * ANT_PITCH
    ant.append(box(ax, (ANT_Y0 + ANT_Y1) / 2, zt, ANT_W, ANT_Y1 - ANT_Y0, -ANT_T))
    if i < ANT_N - 1:
        cy = ANT_Y0 if i % 2 else ANT_Y1
        ant.append(box(ax + ANT_PITCH / 2, cy, zt, ANT_PITCH + ANT_W, ANT_W, -ANT_T))
feed_y = ANT_Y1 + 0.9
ant.append(box(ANT_X0, (ANT_Y1 + feed_y) / 2, zt, ANT_W, feed_y - ANT_Y1 + ANT_W, -ANT_T))
ant.append(box(ANT_X0 + 3.5, feed_y, zt, 7.0, ANT_W, -ANT_T))
module = module.union(union_all(ant))

# castellated half-hole pads along both long edges and the inner end
CAST_R = 0.4
shield_cy = (SHIELD_Y0 + SHIELD_Y1) / 2
cast_pts = []
for k in (-3.5, -2.5, -1.5, -0.5, 0.5, 1.5, 2.5, 3.5):
    py = shield_cy + k * CAST_PITCH
    cast_pts += [(MOD_X0, py), (MOD_X1, py)]
for k in (-2.5, -1.5, -0.5, 0.5, 1.5, 2.5):
    cast_pts.append((mod_cx + k * CAST_PITCH, mod_y0 + MOD_L))
notches = (
    cq.Workplane("XY")
    .workplane(offset=ZB - MOD_T - 0.1)
    .pushPoints(cast_pts)
    .circle(CAST_R)
    .extrude(MOD_T + 0.1 - 0.02)
)
module = module.cut(notches)
# thin solder pads on the module face next to every half-hole
zt = ZB - MOD_T
pads = []
for (px, py) in cast_pts:
    if abs(px - MOD_X0) < 1e-6:
        pads.append(box(px + 0.6, py, zt, 1.0, 0.6, -0.05))
    elif abs(px - MOD_X1) < 1e-6:
        pads.append(box(px - 0.6, py, zt, 1.0, 0.6, -0.05))
    else:
        pads.append(box(px, py - 0.55, zt, 0.6, 0.7, -0.05))
module = module.union(union_all(pads))

# =====================================================================
# micro USB receptacle at the +Y end
# =====================================================================
usb_y1 = BOARD_L / 2 + USB_OVERHANG
usb_cy = usb_y1 - USB_L / 2
# shell: full width at the board, bevelled lower corners (micro-B outline)
usb_prof = [
    (-USB_W / 2, 0.0), (USB_W / 2, 0.0),
    (USB_W / 2, -USB_H + USB_BEVEL), (USB_W / 2 - USB_BEVEL, -USB_H),
    (-USB_W / 2 + USB_BEVEL, -USB_H), (-USB_W / 2, -USB_H + USB_BEVEL),
]
usb = (
    cq.Workplane("XZ", origin=(USB_CX, usb_y1, ZB))
    .polyline(usb_prof).close()
    .extrude(USB_L)
)
# receptacle mouth (same outline, inset) and contact tongue
t = 0.3
mouth_prof = [
    (-USB_W / 2 + t, -t), (USB_W / 2 - t, -t),
    (USB_W / 2 - t, -USB_H + USB_BEVEL + 0.1), (USB_W / 2 - USB_BEVEL - 0.1, -USB_H + t),
    (-USB_W / 2 + USB_BEVEL + 0.1, -USB_H + t), (-USB_W / 2 + t, -USB_H + USB_BEVEL + 0.1),
]
mouth = (
    cq.Workplane("XZ", origin=(USB_CX, usb_y1 + 0.01, ZB))
    .polyline(mouth_prof).close()
    .extrude(USB_MOUTH_D + 0.01)
)
usb = usb.cut(mouth)
tongue = box(USB_CX, usb_y1 - USB_MOUTH_D / 2 - 0.3, ZB - 0.6, 3.8, USB_MOUTH_D - 0.6, -0.6)
usb = usb.union(tongue)

# =====================================================================
# SMD parts on the underside
# =====================================================================
parts = []
# USB-UART bridge, QFN 5x5
qfn = box(2.15, 13.95, ZB, 5.0, 5.0, -0.9).faces("<Z").edges().chamfer(0.2)
parts.append(qfn)

# 3.3 V regulator (moulded body + gull-wing leads on the +X side)
REG_X0, REG_X1, REG_Y0, REG_Y1, REG_H = -0.5, 3.0, 2.2, 7.8, 1.9
reg = (box((REG_X0 + REG_X1) / 2, (REG_Y0 + REG_Y1) / 2, ZB - 0.1,
           REG_X1 - REG_X0, REG_Y1 - REG_Y0, -(REG_H - 0.1))
       .faces("<Z").edges().fillet(0.3))
parts.append(reg)
for ly in (3.45, 5.3, 7.15):
    parts.append(box(REG_X1 + 0.3, ly, ZB - 0.75, 0.8, 0.7, -0.3))    # lead arm
    parts.append(box(REG_X1 + 0.6, ly, ZB, 0.3, 0.7, -1.05))          # lead foot

# input diode (2-terminal, long along Y)
parts.append(box(-6.5, 4.7, ZB, 2.5, 4.0, -1.3))
for ty in (4.7 - 2.4, 4.7 + 2.4):
    parts.append(box(-6.5, ty, ZB, 1.5, 0.8, -0.6))

# SOT-23 parts
def sot23(cx, cy, along_x=True):
    sx, sy = (2.9, 1.3) if along_x else (1.3, 2.9)
    items = [box(cx, cy, ZB - 0.1, sx, sy, -1.0)]
    if along_x:
        for lx, ly in ((cx - 0.95, cy + 1.0), (cx + 0.95, cy + 1.0), (cx, cy - 1.0)):
            items.append(box(lx, ly, ZB, 0.45, 0.8, -0.5))
    else:
        for lx, ly in ((cx + 1.0, cy - 0.95), (cx + 1.0, cy + 0.95), (cx - 1.0, cy)):
            items.append(box(lx, ly, ZB, 0.8, 0.45, -0.5))
    return union_all(items)

parts.append(sot23(7.7, 6.9, True))
parts.append(sot23(7.7, 12.6, True))

# flat square part and small chip parts
parts.append(box(-3.45, 5.6, ZB, 2.6, 2.6, -0.35))
parts.append(box(-6.8, 14.0, ZB, 2.0, 1.25, -0.6))
parts.append(box(-3.2, 12.0, ZB, 2.0, 1.25, -0.6))

# two rows of 0603 passives
GRID_N = 9
GRID_X0, GRID_X1 = -8.6, 9.8
gp = (GRID_X1 - GRID_X0) / GRID_N
for i in range(GRID_N):
    cx = GRID_X0 + gp * (i + 0.5)
    for cy in (9.15, 10.2):
        parts.append(box(cx, cy, ZB, gp - 0.2, 0.9, -0.45))

# reset / flash tactile switches beside the USB
for (bx, by) in BUTTONS:
    sw = box(bx, by, ZB, BTN_W, BTN_L, -BTN_H).edges("|Z").chamfer(0.4)
    sw = sw.union(cq.Workplane("XY").workplane(offset=ZB - BTN_H).circle(BTN_ACT_D / 2).extrude(-BTN_ACT_H).translate((bx, by, 0)))
    for dx in (-0.9, 0.9):
        for dy in (-1, 1):
            sw = sw.union(box(bx + dx, by + dy * (BTN_L / 2 + 0.2), ZB, 0.5, 0.6, -0.35))
    parts.append(sw)

smd = union_all(parts)

result = (board.union(headers, clean=False).union(module, clean=False)
          .union(usb, clean=False).union(smd, clean=False))
